import cadquery as cq

# ============================================================
#  Rounded base pad with a raised, point-symmetric "Z" plate
#  on top and four blind holes in the underside.
# ============================================================

# ---------------- driving dimensions (mm) ----------------
BASE_L = 100.0        # base length along X
BASE_W = 86.9         # base width along Y
BASE_H = 11.3         # base height (bottom face to flat top)
CORNER_R = 10.5       # plan-view corner radius of the base
TOP_FILLET = 7.3      # rounded top edge of the base

PLATE_T = 3.9         # raised plate thickness
PLATE_HX = 37.4       # plate half extent in X
PLATE_HY = 32.2       # plate half extent in Y
STEP_X = 24.65        # |x| of the narrow (stepped-in) edges
NOTCH_Y_HI = 9.3      # |y| where each slanted edge leaves the stepped edge
NOTCH_Y_LO = 20.9     # |y| where each slanted edge meets the full-width edge

HOLE_D = 8.7          # blind holes in the underside
HOLE_DEPTH = 6.0
HOLE_INSET = 8.4      # hole centre distance from the outer side faces

# ---------------- base pad ----------------
base = (
    cq.Workplane("XY")
    .sketch()
    .rect(BASE_L, BASE_W)
    .vertices()
    .fillet(CORNER_R)
    .finalize()
    .extrude(BASE_H)
)
base = base.faces(">Z").edges().fillet(TOP_FILLET)

# ---------------- raised plate ----------------
# Outline is symmetric under a 180 deg rotation about Z:
# the +X side is stepped in at the top (+Y), the -X side at the bottom (-Y),
# each joined to the full-width edge by a slanted face.
pts = [
    (-PLATE_HX, PLATE_HY),
    (STEP_X, PLATE_HY),
    (STEP_X, NOTCH_Y_HI),
    (PLATE_HX, -NOTCH_Y_LO),
    (PLATE_HX, -PLATE_HY),
    (-STEP_X, -PLATE_HY),
    (-STEP_X, -NOTCH_Y_HI),
    (-PLATE_HX, NOTCH_Y_LO),
]
plate = (
    cq.Workplane("XY", origin=(0, 0, BASE_H))
    .polyline(pts)
    .close()
    .extrude(PLATE_T)
)

part = base.union(plate)

# ---------------- blind holes from the underside ----------------
hx = BASE_L / 2 - HOLE_INSET
hy = BASE_W / 2 - HOLE_INSET
part = (
    part.faces("<Z")
    .workplane(centerOption="CenterOfBoundBox")
    .rect(2 * hx, 2 * hy, forConstruction=True)
    .vertices()
    .hole(HOLE_D, HOLE_DEPTH)
)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
